import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 70.0            # overall length along X (tab tip to +X end)
W = 49.2            # overall width along Y (outer faces of the thick plate parts)
H = 28.3            # overall height of the side plates
T_THICK = 5.35      # side plate thickness, +X (outer) half
T_THIN = 3.4        # side plate thickness, -X (pin) half, inner face flush
STEP_X = 33.3       # x where the plate steps from thin to thick
TOP_FLAT_END = 40.9 # end of flat top, start of the slope towards +X
END_H = 15.1        # plate height at the +X end
SLOPE_FILLET = 2.0  # rounding between flat top and slope

# pin end (tab) geometry
TAB_TIP_BOT = (0.0, 11.47)
TAB_TIP_TOP = (1.64, 24.45)
TAB_TOP_END = 10.6           # x where tab top meets chamfer
TAB_CH_END = 14.5            # x where chamfer reaches full height
PIN_X = 19.06
PIN_Z = 14.1
PIN_D = 11.2
PIN_PROUD = 1.1              # pin protrudes beyond the thick plate outer face
ARC_R = PIN_Z                # bottom round of the tab, centred on the pin
ARC_END_ANG = 195.5          # deg, end of the bottom arc (stop face start)

# floor
FLOOR_T = 5.67
FLOOR_X_BOT = 22.1           # floor starts here at the bottom ...
FLOOR_X_TOP = 27.8           # ... and here at the top (45 deg bevel)

# countersunk mounting slots
SLOT_XS = (36.6, 55.4)
SLOT_W = 5.8                 # along X
SLOT_LEN = 11.0              # along Y (overall)
CSK = 2.9                    # 45 deg countersink size

Y_IN = W / 2.0 - T_THICK     # inner face of side plates (|y|)


def plate_profile():
    """Side-plate outline in the XZ plane (x, z)."""
    a_end = math.radians(ARC_END_ANG)
    a_mid = math.radians((270.0 + ARC_END_ANG) / 2.0)
    p_arc_end = (PIN_X + ARC_R * math.cos(a_end), PIN_Z + ARC_R * math.sin(a_end))
    p_arc_mid = (PIN_X + ARC_R * math.cos(a_mid), PIN_Z + ARC_R * math.sin(a_mid))
    wp = (
        cq.Workplane("XZ")
        .moveTo(*TAB_TIP_BOT)
        .lineTo(*TAB_TIP_TOP)
        .lineTo(TAB_TOP_END, TAB_TIP_TOP[1])
        .lineTo(TAB_CH_END, H)
        .lineTo(TOP_FLAT_END, H)
        .lineTo(L, END_H)
        .lineTo(L, 0.0)
        .lineTo(PIN_X, 0.0)
        .threePointArc(p_arc_mid, p_arc_end)
        .close()
    )
    return wp


def side_plate(sign):
    """sign=+1 -> +Y plate, sign=-1 -> -Y plate."""
    # XZ workplane extrudes towards -Y; build for +Y side then mirror
    thin = plate_profile().extrude(-T_THIN)          # y: 0 .. T_THIN
    thick_clip = (
        cq.Workplane("XY")
        .box(L - STEP_X, T_THICK, H + 2, centered=False)
        .translate((STEP_X, 0, -1))
    )
    thick = plate_profile().extrude(-T_THICK).intersect(thick_clip)
    plate = thin.union(thick)
    # pin boss
    boss_len = (T_THICK + PIN_PROUD) - T_THIN
    boss = (
        cq.Workplane("XZ", origin=(0, T_THIN, 0))
        .center(PIN_X, PIN_Z)
        .circle(PIN_D / 2.0)
        .extrude(-boss_len)
        # turn the cylinder seam to the underside (cosmetic only)
        .rotate((PIN_X, 0, PIN_Z), (PIN_X, 1, PIN_Z), 90)
    )
    plate = plate.union(boss)
    plate = plate.translate((0, Y_IN, 0))
    if sign < 0:
        plate = plate.mirror("XZ")
    return plate


# floor with 45 deg bevel at the -X end
floor = (
    cq.Workplane("XZ")
    .polyline([(FLOOR_X_BOT, 0.0), (L, 0.0), (L, FLOOR_T), (FLOOR_X_TOP, FLOOR_T)])
    .close()
    .extrude(Y_IN + 0.5, both=True)
)

body = floor.union(side_plate(+1)).union(side_plate(-1))

# rounding between flat top and slope of the thick plate parts
if SLOPE_FILLET > 0:
    body = body.edges(
        cq.selectors.BoxSelector(
            (TOP_FLAT_END - 0.5, -W, H - 0.5), (TOP_FLAT_END + 0.5, W, H + 0.5)
        )
    ).fillet(SLOPE_FILLET)

# countersunk slots through the floor
for sx in SLOT_XS:
    thru = (
        cq.Workplane("XY", origin=(sx, 0, -1))
        .slot2D(SLOT_LEN, SLOT_W, angle=90)
        .extrude(FLOOR_T + 2)
    )
    csk = (
        cq.Workplane("XY", origin=(sx, 0, FLOOR_T))
        .slot2D(SLOT_LEN + 2 * CSK, SLOT_W + 2 * CSK, angle=90)
        .extrude(-CSK, taper=45)
    )
    body = body.cut(thru).cut(csk)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
